import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Parallel-link robot gripper: body block with a D-shaped mounting lug, two
# trapezoid side plates joined by spacer / pivot rods, two pairs of links and
# two fingers (the same finger part, mounted flipped on the lower jaw).
# Coordinates: X along the arm (gripper toward +X), Z up, Y across.
# Origin: X = body end face, Y = body front (-Y) face, Z = mechanism centre.
# ---------------------------------------------------------------------------

VIEW = {"azimuth": 45, "elevation": 26}

# body block
BODY_L = 112.0
BODY_W = 45.0          # Y
BODY_H = 41.35         # Z
BODY_ZC = 0.22         # body centre height above the mechanism centre

# mounting lug (D-shaped ear with a vertical bore, taller than the body)
LUG_W = 50.0           # X width where it joins the body
LUG_R = 22.8           # round-end radius
LUG_CX = -85.0         # bore centre X
LUG_CY = -20.7         # bore centre Y
LUG_H = 47.1           # Z height
LUG_BORE_R = 14.9

# side plates (trapezoids seen from the front)
PL_L = 59.8
PL_H0 = 39.6           # height at the body
PL_H1 = 29.25          # height at the free end
PL_ZC = 0.36           # plate centre height above the mechanism centre
PL_T = 4.3
PL_FRONT_Y = 10.5      # front plate outer face
PL_BACK_Y = 29.5       # back plate inner face

# links / fingers (stacked between the plates, links next to the front plate)
LINK_T = 2.9
LINK_R = 4.4           # rounded link ends
FING_T = 4.1
FING_R_UP = 5.3        # rounded finger heel radius (upper / lower)
FING_R_LO = 4.8
PIN_R = 2.3            # pivot bore through link ends and fingers
RAB_W = 1.6            # rabbet width that leaves a thin gripping lip at the tips

# rods between the plates (x, z, r); their ends show as circles in the plates
RODS = [
    (3.95, 13.35, 1.9),
    (3.95, -13.35, 1.9),
    (26.3, 8.9, 2.6),
    (26.3, -8.9, 2.6),
    (48.95, 5.25, 2.5),
    (48.95, -5.25, 2.5),
    (56.4, -0.15, 2.0),
]
HOLE_DEPTH = 0.3       # pin ends sit almost flush in the plates

# linkage pivots (X, Z): plate pivots share the rods, finger pivots at link tops
A_UP, B_UP = (26.3, 8.9), (48.95, 5.25)
A_LO, B_LO = (26.3, -8.9), (48.95, -5.25)
P1, P2 = (51.5, 37.0), (71.5, 34.95)       # upper finger pivots
P3, P4 = (56.3, -31.55), (76.8, -30.15)    # lower finger pivots

# finger outlines (X, Z)
UP_INNER_START = (76.3, 30.3)
UP_INNER = [(81.7, 29.15), (89.4, 27.25), (97.1, 25.25), (104.85, 23.75),
            (112.0, 23.1), (119.2, 22.2)]
UP_TIP = (119.6, 25.9)
UP_TOP_FAR = (104.1, 37.4)
UP_RABBET = [(96.0, 25.54), (104.85, 24.4), (112.0, 24.1), (122.0, 23.9)]

LO_BOT_FAR = (109.1, -33.15)
LO_TIP = (124.8, -22.6)
LO_TIP_TOP = (124.3, -18.75)
LO_INNER = [(117.6, -18.8), (106.0, -19.3), (96.7, -20.55), (86.7, -23.15),
            (79.8, -23.95)]
LO_INNER_END_DZ = 5.9
LO_RABBET = [(86.7, -23.1), (96.7, -21.35), (106.0, -20.5), (115.0, -20.3), (127.0, -20.4)]


# ---------------------------------------------------------------- helpers
def xz_prism(wp_builder, y0, y1):
    """wp_builder(workplane) -> closed wire drawn in (X, Z); extruded from y0 to y1."""
    wp = cq.Workplane("XZ", origin=(0, y0, 0))
    return wp_builder(wp).extrude(-(y1 - y0))


def tangent_point(ext, c, r, side):
    """Tangent point on circle (c, r) of a line through the external point ext."""
    dx, dz = ext[0] - c[0], ext[1] - c[1]
    d = math.hypot(dx, dz)
    a = math.atan2(dz, dx) + side * math.acos(r / d)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a)), a


def arc_mid(c, r, a0, a1):
    while a1 < a0:
        a1 += 2 * math.pi
    am = (a0 + a1) / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def stadium(p, q, r, y0, y1):
    """Link bar with fully rounded ends between pivots p and q."""
    dx, dz = q[0] - p[0], q[1] - p[1]
    L = math.hypot(dx, dz)
    ux, uz = dx / L, dz / L
    nx, nz = -uz, ux
    p_a, p_b = (p[0] + nx * r, p[1] + nz * r), (p[0] - nx * r, p[1] - nz * r)
    q_a, q_b = (q[0] + nx * r, q[1] + nz * r), (q[0] - nx * r, q[1] - nz * r)
    p_m, q_m = (p[0] - ux * r, p[1] - uz * r), (q[0] + ux * r, q[1] + uz * r)

    def build(wp):
        return (wp.moveTo(*p_b).lineTo(*q_b).threePointArc(q_m, q_a)
                .lineTo(*p_a).threePointArc(p_m, p_b).close())
    return xz_prism(build, y0, y1)


# ---------------------------------------------------------------- body + lug
body = (cq.Workplane("XY").box(BODY_L, BODY_W, BODY_H)
        .translate((-BODY_L / 2, BODY_W / 2, BODY_ZC)))

lug_x0 = -BODY_L
lug_x1 = -BODY_L + LUG_W
lug_tan, _ = tangent_point((lug_x0, 0.0), (LUG_CX, LUG_CY), LUG_R, +1)
lug = (cq.Workplane("XY", origin=(0, 0, -LUG_H / 2))
       .moveTo(lug_x0, 0.0)
       .lineTo(*lug_tan)
       .threePointArc((LUG_CX, LUG_CY - LUG_R), (LUG_CX + LUG_R, LUG_CY))
       .lineTo(lug_x1, 0.0)
       .close()
       .extrude(LUG_H))
lug = lug.cut(cq.Workplane("XY", origin=(LUG_CX, LUG_CY, -LUG_H))
              .circle(LUG_BORE_R).extrude(2 * LUG_H))

result = body.union(lug)

# ---------------------------------------------------------------- side plates
plate_pts = [(0.0, PL_ZC - PL_H0 / 2), (PL_L, PL_ZC - PL_H1 / 2),
             (PL_L, PL_ZC + PL_H1 / 2), (0.0, PL_ZC + PL_H0 / 2)]


def side_plate(y0, y1, outer_y, outward):
    pl = xz_prism(lambda wp: wp.polyline(plate_pts).close(), y0, y1)
    for (x, z, r) in RODS:
        if outward < 0:
            ya, yb = outer_y - 0.01, outer_y + HOLE_DEPTH
        else:
            ya, yb = outer_y - HOLE_DEPTH, outer_y + 0.01
        pl = pl.cut(xz_prism(lambda wp, x=x, z=z, r=r: wp.center(x, z).circle(r * 1.05), ya, yb))
    return pl


front_plate = side_plate(PL_FRONT_Y, PL_FRONT_Y + PL_T, PL_FRONT_Y, -1)
back_plate = side_plate(PL_BACK_Y, PL_BACK_Y + PL_T, PL_BACK_Y + PL_T, +1)
result = result.union(front_plate).union(back_plate)

# ---------------------------------------------------------------- rods
for (x, z, r) in RODS:
    rod = xz_prism(lambda wp, x=x, z=z, r=r: wp.center(x, z).circle(r),
                   PL_FRONT_Y + PL_T - 0.2, PL_BACK_Y + 0.2)
    result = result.union(rod)

# ---------------------------------------------------------------- links
LY0 = PL_FRONT_Y + PL_T
LY1 = LY0 + LINK_T
for (p, q) in [(A_UP, P1), (B_UP, P2), (A_LO, P3), (B_LO, P4)]:
    result = result.union(stadium(p, q, LINK_R, LY0 - 0.05, LY1))

# ---------------------------------------------------------------- fingers
FY0 = LY1
FY1 = FY0 + FING_T


def finger_upper():
    R = FING_R_UP
    tb, a_b = tangent_point(UP_INNER_START, P1, R, -1)
    tt, a_t = tangent_point(UP_TOP_FAR, P1, R, +1)
    mid = arc_mid(P1, R, a_t, a_b)

    def build(wp):
        t0 = (UP_INNER_START[0] - tb[0], UP_INNER_START[1] - tb[1])
        return (wp.moveTo(*tb).lineTo(*UP_INNER_START)
                .spline(UP_INNER, tangents=[t0, (1.0, -0.08)], includeCurrent=True)
                .lineTo(*UP_TIP).lineTo(*UP_TOP_FAR).lineTo(*tt)
                .threePointArc(mid, tb).close())
    f = xz_prism(build, FY0 - 0.05, FY1)

    # rabbet on the link (-Y) side of the inner edge leaves a thin gripping lip
    def rab(wp):
        return (wp.moveTo(*UP_RABBET[0])
                .spline(UP_RABBET[1:], tangents=[(1.0, -0.19), (1.0, -0.01)], includeCurrent=True)
                .lineTo(UP_RABBET[-1][0], 18.0).lineTo(UP_RABBET[0][0], 18.0).close())
    return f.cut(xz_prism(rab, FY0 - 0.2, FY0 + RAB_W))


def finger_lower():
    R = FING_R_LO
    inner_end = (P4[0], P4[1] + LO_INNER_END_DZ)
    tb, a_b = tangent_point(LO_BOT_FAR, P3, R, -1)
    tt, a_t = tangent_point(inner_end, P3, R, +1)
    mid = arc_mid(P3, R, a_t, a_b)

    def build(wp):
        t1 = (tt[0] - inner_end[0], tt[1] - inner_end[1])
        return (wp.moveTo(*tb).lineTo(*LO_BOT_FAR).lineTo(*LO_TIP).lineTo(*LO_TIP_TOP)
                .spline(LO_INNER + [inner_end], tangents=[(-1.0, 0.0), t1], includeCurrent=True)
                .lineTo(*tt)
                .threePointArc(mid, tb).close())
    f = xz_prism(build, FY0 - 0.05, FY1)

    # same finger part mounted flipped: lip on the -Y side, rabbet on the +Y side
    def rab(wp):
        return (wp.moveTo(*LO_RABBET[0])
                .spline(LO_RABBET[1:], tangents=[(1.0, 0.2), (1.0, -0.01)], includeCurrent=True)
                .lineTo(LO_RABBET[-1][0], -14.0).lineTo(LO_RABBET[0][0], -14.0).close())
    return f.cut(xz_prism(rab, FY1 - RAB_W, FY1 + 0.2))


result = result.union(finger_upper()).union(finger_lower())

# pivot bores through link ends and fingers
for p in (P1, P2, P3, P4):
    result = result.cut(xz_prism(lambda wp, p=p: wp.center(*p).circle(PIN_R), LY0 - 0.1, FY1 + 0.1))
